import math
import cadquery as cq
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
from OCP.GC import GC_MakeArcOfCircle, GC_MakeSegment
from OCP.GeomConvert import GeomConvert, GeomConvert_CompCurveToBSplineCurve
from OCP.gp import gp_Pnt

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------------------------------------------------------------------
# Servo arm link: a round horn end (-X) and a servo box (+X).  Two plates with
# a tapered outline are joined by four pie-shaped standoffs around the horn
# pattern, a transverse rib and the closed servo box.  The servo body shows
# through a rectangular opening in the top and protrudes below the box with
# its output horn.
# Origin at the horn-pattern centre of the round end, Z=0 at the bottom face.
# ---------------------------------------------------------------------------

# overall / outline
R_END = 34.75            # radius of the round end
BOX_X0 = 146.5           # -X face of servo box
BOX_X1 = 202.5           # +X end of the link
Y_POS_END = 23.2         # +Y edge at the +X end (edge tapers from round end)
Y_NEG = -64.0            # -Y face of the servo box
H = 55.0                 # overall height of link body
T_TOP = 3.8              # top plate thickness
T_BOT = 3.2              # bottom plate thickness
R_BLEND = 15.0           # blend radius where the tapered -Y side meets the box side

# web
R_ARC2 = 43.5            # outer radius of the +X standoffs
CORE_R = 5.3             # open core at the centre of the standoffs
POST_R_OUT = R_END + 3.0 # -X standoffs run out to the plate outline (flush)
RIB_X0, RIB_X1 = 67.4, 76.2
SECTORS = [              # (start deg, end deg, outer radius); mirror-symmetric about X
    (120.0, 151.5, POST_R_OUT),
    (208.5, 240.0, POST_R_OUT),
    (299.0, 331.5, R_ARC2),
    (28.5, 61.0, R_ARC2),
]

# holes
HOLE_PCD_R = 19.3
CB_D, CB_DEPTH, CB_THRU = 9.6, 3.0, 5.0
SMALL_D = 5.0
BOT_CENTER_D = 21.6
BOT_HOLE_D = 5.0
BOX_HOLE_D = 5.2
BOX_HOLE_Y = (-47.55, -6.25)
BOX_HOLE_Z = (21.5, 42.2)

# servo inside the box
SERVO_X0, SERVO_X1 = 149.8, 200.0
SERVO_Y0, SERVO_Y1 = -60.4, 20.8
POCKET_X0, POCKET_X1 = 149.4, 200.4
POCKET_Y0, POCKET_Y1 = -62.3, 21.4
POCKET_DEPTH = 8.0
SERVO_CHAMFER = 3.2
SERVO_TOP_RECESS = 0.5
SERVO_BOTTOM_DROP = 4.0

# horn
HORN_X, HORN_Y = 174.5, 1.9
HORN_D, HORN_T = 34.7, 3.6
HORN_HOLE_PCD_R, HORN_HOLE_D = 14.0, 3.2
SHAFT_HOLE_D = 2.6
HUB_D, HUB_T = 13.4, 3.4
SHAFT_D, SHAFT_T = 6.8, 3.8


def tangent_point(px, py, r, upper):
    """Tangent point on circle (0,0,r) of a line through external point P."""
    d = math.hypot(px, py)
    base = math.atan2(py, px)
    off = math.acos(r / d)
    a = base + off if upper else base - off
    return (r * math.cos(a), r * math.sin(a))


TAN_TOP = tangent_point(BOX_X1, Y_POS_END, R_END, True)
TAN_BOT = tangent_point(BOX_X0, Y_NEG, R_END, False)


def _fillet_pts(p_prev, corner, p_next, r):
    """Tangent points and mid point of a blend arc of radius r at a 2D corner."""
    ax, ay = p_prev[0] - corner[0], p_prev[1] - corner[1]
    bx, by = p_next[0] - corner[0], p_next[1] - corner[1]
    la, lb = math.hypot(ax, ay), math.hypot(bx, by)
    ax, ay, bx, by = ax / la, ay / la, bx / lb, by / lb
    half = 0.5 * math.acos(ax * bx + ay * by)
    t = r / math.tan(half)
    t1 = (corner[0] + ax * t, corner[1] + ay * t)
    t2 = (corner[0] + bx * t, corner[1] + by * t)
    mx, my = ax + bx, ay + by
    lm = math.hypot(mx, my)
    dc = r / math.sin(half)
    c = (corner[0] + mx / lm * dc, corner[1] + my / lm * dc)
    m = (c[0] - mx / lm * r, c[1] - my / lm * r)
    return t1, m, t2


def outline_wire():
    """Closed outline: one smooth (exact NURBS) curve for the -Y side, the round
    end and the +Y side, closed by the straight +X end of the servo box."""
    def P(p):
        return gp_Pnt(p[0], p[1], 0.0)

    c_neg = (BOX_X0, Y_NEG)
    b1, bm, b2 = _fillet_pts((BOX_X1, Y_NEG), c_neg, TAN_BOT, R_BLEND)
    curves = [
        GC_MakeSegment(P((BOX_X1, Y_NEG)), P(b1)).Value(),
        GC_MakeArcOfCircle(P(b1), P(bm), P(b2)).Value(),
        GC_MakeSegment(P(b2), P(TAN_BOT)).Value(),
        GC_MakeArcOfCircle(P(TAN_BOT), P((-R_END, 0.0)), P(TAN_TOP)).Value(),
        GC_MakeSegment(P(TAN_TOP), P((BOX_X1, Y_POS_END))).Value(),
    ]
    comp = GeomConvert_CompCurveToBSplineCurve(GeomConvert.CurveToBSplineCurve_s(curves[0]))
    for crv in curves[1:]:
        comp.Add(GeomConvert.CurveToBSplineCurve_s(crv), 1e-7, True)
    side = cq.Edge(BRepBuilderAPI_MakeEdge(comp.BSplineCurve()).Edge())
    end = cq.Edge.makeLine(cq.Vector(BOX_X1, Y_POS_END, 0), cq.Vector(BOX_X1, Y_NEG, 0))
    return cq.Wire.assembleEdges([side, end])


def outline(z0, h):
    face = cq.Face.makeFromWires(outline_wire())
    solid = cq.Solid.extrudeLinear(face, cq.Vector(0, 0, h)).translate(cq.Vector(0, 0, z0))
    return cq.Workplane("XY").add(solid)


def pol(r, deg):
    a = math.radians(deg)
    return (r * math.cos(a), r * math.sin(a))


def sector(r_in, r_out, a0, a1, z0, h):
    am = 0.5 * (a0 + a1)
    wp = (
        cq.Workplane("XY", origin=(0, 0, z0))
        .moveTo(*pol(r_out, a0))
        .threePointArc(pol(r_out, am), pol(r_out, a1))
        .lineTo(*pol(r_in, a1))
        .threePointArc(pol(r_in, am), pol(r_in, a0))
        .close()
    )
    return wp.extrude(h)


def xslab(x0, x1):
    return cq.Workplane("XY").box(x1 - x0, 400, 400, centered=(False, True, True)).translate((x0, 0, 0))


# ---------------------------------------------------------------------------
# body: full outline prism, hollowed between the plates except for the servo
# box, the transverse rib and four pie-shaped standoffs around the horn pattern
# (one per diagonal bolt hole); the open windows lie on the 0/90/180/270 deg
# directions and there is a small open core at the centre.
# ---------------------------------------------------------------------------
prism = outline(0.0, H)

z_c0, z_c1 = T_BOT, H - T_TOP
cavity = (
    cq.Workplane("XY")
    .box(400, 300, z_c1 - z_c0, centered=(True, True, False))
    .translate((100, 0, z_c0))
)
keep_box = (
    cq.Workplane("XY")
    .box(BOX_X1 - BOX_X0 + 5, Y_POS_END - Y_NEG + 5, H, centered=False)
    .translate((BOX_X0, Y_NEG - 5, 0))
)
keep_rib = xslab(RIB_X0, RIB_X1)
cavity = cavity.cut(keep_box).cut(keep_rib)
for (a0, a1, r_out) in SECTORS:
    cavity = cavity.cut(sector(CORE_R, r_out, a0, a1, -1.0, H + 2.0))

body = prism.cut(cavity)

# ---------------------------------------------------------------------------
# holes in the round end
# ---------------------------------------------------------------------------
# top plate: 4 counterbored + 4 plain holes
for ang in (0, 90, 180, 270):
    x, y = pol(HOLE_PCD_R, ang)
    cb = cq.Workplane("XY", origin=(x, y, H - CB_DEPTH)).circle(CB_D / 2).extrude(CB_DEPTH + 1)
    th = cq.Workplane("XY", origin=(x, y, H - T_TOP - 0.5)).circle(CB_THRU / 2).extrude(T_TOP + 1)
    body = body.cut(cb).cut(th)
for ang in (45, 135, 225, 315):
    x, y = pol(HOLE_PCD_R, ang)
    th = cq.Workplane("XY", origin=(x, y, H - T_TOP - 0.5)).circle(SMALL_D / 2).extrude(T_TOP + 1)
    bolt = cq.Workplane("XY", origin=(x, y, -1)).circle(BOT_HOLE_D / 2).extrude(H + 2)
    body = body.cut(th).cut(bolt)

# bottom plate: large centre hole + 8 holes
body = body.cut(cq.Workplane("XY", origin=(0, 0, -1)).circle(BOT_CENTER_D / 2).extrude(T_BOT + 1))
for k in range(8):
    x, y = pol(HOLE_PCD_R, 45 * k)
    body = body.cut(cq.Workplane("XY", origin=(x, y, -1)).circle(BOT_HOLE_D / 2).extrude(T_BOT + 1))

# ---------------------------------------------------------------------------
# servo box: top opening with recessed servo top, bottom protrusion, horn
# ---------------------------------------------------------------------------
pocket = (
    cq.Workplane("XY", origin=(0, 0, H - POCKET_DEPTH))
    .center((POCKET_X0 + POCKET_X1) / 2, (POCKET_Y0 + POCKET_Y1) / 2)
    .rect(POCKET_X1 - POCKET_X0, POCKET_Y1 - POCKET_Y0)
    .extrude(POCKET_DEPTH + 1)
)
body = body.cut(pocket)


def servo_block(z0, h):
    return (
        cq.Workplane("XY", origin=(0, 0, z0))
        .center((SERVO_X0 + SERVO_X1) / 2, (SERVO_Y0 + SERVO_Y1) / 2)
        .rect(SERVO_X1 - SERVO_X0, SERVO_Y1 - SERVO_Y0)
        .extrude(h)
        .edges("|Z")
        .chamfer(SERVO_CHAMFER)
    )


# servo body visible through the top opening (slightly recessed)
body = body.union(servo_block(H - POCKET_DEPTH - 0.5, POCKET_DEPTH + 0.5 - SERVO_TOP_RECESS))
# servo body protruding below the box
body = body.union(servo_block(-SERVO_BOTTOM_DROP, SERVO_BOTTOM_DROP + 0.5))

z_h0 = -SERVO_BOTTOM_DROP
horn = (
    cq.Workplane("XY", origin=(HORN_X, HORN_Y, z_h0 - HORN_T))
    .circle(HORN_D / 2)
    .extrude(HORN_T + 0.01)
)
horn = horn.cut(
    cq.Workplane("XY", origin=(HORN_X, HORN_Y, z_h0 - HORN_T - 1))
    .polarArray(HORN_HOLE_PCD_R, 0, 360, 8)
    .circle(HORN_HOLE_D / 2)
    .extrude(HORN_T + 0.5)
)
hub = (
    cq.Workplane("XY", origin=(HORN_X, HORN_Y, z_h0 - HORN_T - HUB_T))
    .circle(HUB_D / 2)
    .extrude(HUB_T + 0.01)
)
shaft = (
    cq.Workplane("XY", origin=(HORN_X, HORN_Y, z_h0 - HORN_T - HUB_T - SHAFT_T))
    .circle(SHAFT_D / 2)
    .extrude(SHAFT_T + 0.01)
)
shaft = shaft.cut(
    cq.Workplane("XY", origin=(HORN_X, HORN_Y, z_h0 - HORN_T - HUB_T - SHAFT_T - 1))
    .circle(SHAFT_HOLE_D / 2)
    .extrude(3.5)
)
body = body.union(horn).union(hub).union(shaft)

# box side holes (+X and -X faces)
for yy in BOX_HOLE_Y:
    for zz in BOX_HOLE_Z:
        hx = cq.Workplane("YZ", origin=(BOX_X1 - 3.0, yy, zz)).circle(BOX_HOLE_D / 2).extrude(4.0)
        hx2 = cq.Workplane("YZ", origin=(BOX_X0 - 1.0, yy, zz)).circle(BOX_HOLE_D / 2).extrude(4.0)
        body = body.cut(hx).cut(hx2)

result = body
